import cadquery as cq
import math

# ======================================================================
#  Drafted cover plate with an eroded (fracture-like) channel across it.
#  The part is a thin-walled cover, open underneath: the underside
#  follows the top surface (channel appears as a ridge inside).
# ======================================================================

# ---------------- driving dimensions (mm) ----------------
W = 75.5          # plate width  (X)
L = 100.0         # plate length (Y)
T = 5.45          # plate height (Z)
DRAFT_IN = 0.92   # inward offset of the top outline relative to the bottom
CORNER_C = 1.7    # corner chamfer of the bottom outline
CORNER_C_TOP = 0.9  # corner chamfer of the top outline (facets taper upward)

WALL = 0.5        # wall / skin thickness of the cover (0 -> solid plate)

GROOVE_D = 2.6    # depth of the eroded channel below the top face
MARGIN = 0.6      # channel tool extends this far above the top face
MIN_FLOOR = 0.6   # minimum floor width of the channel
SHOULDER_R_LEFT = 1.5   # rounded shoulder on the -X side of the channel
SHOULDER_R_RIGHT = 1.2  # rounded shoulder on the +X side of the channel

# steeper portion of the -X side face near the back (+Y) corner
STEP_Y = 41.5     # where the steeper face portion begins (45 deg transition)
STEP_IN = 1.0     # additional inset of its top edge beyond the normal draft

# crease lines of the channel as seen from above: (y, x_left, x_right)
CREASES = [
    (-56.0, -12.9, 1.1), (-49.1, -12.5, 1.1), (-44.0, -11.8, 1.3),
    (-37.0, -10.7, 3.3), (-30.0, -9.4, 3.5), (-25.0, -7.0, 2.5),
    (-21.0, -3.3, 1.0), (-17.5, -0.8, 1.0), (-13.0, -1.3, 2.0),
    (-8.0, 0.0, 3.3), (-3.0, 0.6, 3.6), (1.0, 1.1, 4.9),
    (5.0, 1.6, 6.1), (9.0, 0.0, 8.9), (12.5, -1.3, 11.2),
    (17.0, -0.7, 12.5), (25.0, 1.0, 14.2), (33.0, 2.0, 15.4),
    (41.5, 3.5, 17.4), (49.1, 5.1, 18.3), (56.0, 6.0, 19.0),
]


def profile(y):
    """(shoulder offset left, shoulder offset right, left bank run, right bank run).
    Inside the plate the rounded shoulders sit outside the crease lines;
    at the cut ends the channel walls are crisp."""
    if y <= -49.0:
        return 1.0, 0.4, 1.5, 5.5
    if y <= -44.0:
        return 1.8, 1.2, 2.5, 4.0
    if y >= 49.0:
        return 0.5, 0.3, 1.5, 4.3
    if y >= 41.5:
        return 1.8, 1.2, 2.6, 3.6
    return 2.3, 1.8, 3.3, 2.8


# channel stations: (y, x_left_top, x_right_top, left_run, right_run)
STATIONS = []
for _y, _xl, _xr in CREASES:
    _ol, _or, _sl, _sr = profile(_y)
    _run = (_xr + _or) - (_xl - _ol) - MIN_FLOOR
    if _sl + _sr > _run:  # narrow neck: scale both banks to keep a small floor
        _f = max(_run, 0.2) / (_sl + _sr)
        _sl, _sr = _sl * _f, _sr * _f
    STATIONS.append((_y, _xl - _ol, _xr + _or, _sl, _sr))

# ---------------- helpers ----------------
cos_t = math.cos(math.atan2(DRAFT_IN, T))
hw, hl = W / 2.0, L / 2.0


def outline_at(z):
    """Outer plate outline at height z (the side faces and corner facets are
    planar, so every vertex moves linearly between the bottom and top outline)."""
    cb, ct, d = CORNER_C, CORNER_C_TOP, DRAFT_IN
    bot = [
        (-hw + cb, -hl), (hw - cb, -hl), (hw, -hl + cb), (hw, hl - cb),
        (hw - cb, hl), (-hw + cb, hl), (-hw, hl - cb), (-hw, -hl + cb),
    ]
    a, b = hw - d, hl - d
    top = [
        (-a + ct, -b), (a - ct, -b), (a, -b + ct), (a, b - ct),
        (a - ct, b), (-a + ct, b), (-a, b - ct), (-a, -b + ct),
    ]
    s = z / T
    return [(xb + (xt - xb) * s, yb + (yt - yb) * s) for (xb, yb), (xt, yt) in zip(bot, top)]


def inset_polygon(pts, delta):
    """Move every edge of a convex CCW polygon inward by delta (sharp corners)."""
    n = len(pts)
    lines = []
    for i in range(n):
        (x1, y1), (x2, y2) = pts[i], pts[(i + 1) % n]
        dx, dy = x2 - x1, y2 - y1
        ln = math.hypot(dx, dy)
        nx, ny = -dy / ln, dx / ln                     # inward normal (left side)
        lines.append(((x1 + nx * delta, y1 + ny * delta), (dx, dy)))
    out = []
    for i in range(n):
        (p1, d1), (p2, d2) = lines[i - 1], lines[i]
        den = d1[0] * d2[1] - d1[1] * d2[0]
        t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
        out.append((p1[0] + d1[0] * t, p1[1] + d1[1] * t))
    return out


def slab(inset, z0, z1):
    """Drafted slab with chamfered corners between heights z0 and z1; its side
    faces are the outer side faces moved inward by 'inset' (horizontally)."""
    rings = []
    for z in (z0, z1):
        pts = inset_polygon(outline_at(z), inset) if inset else outline_at(z)
        rings.append([cq.Vector(x, y, z) for x, y in pts])
    lo, hi = rings
    n = len(lo)

    def planar(pts):
        return cq.Face.makeFromWires(cq.Wire.makePolygon(pts, close=True))

    faces = [planar(list(reversed(lo))), planar(hi)]
    for i in range(n):
        j = (i + 1) % n
        faces.append(planar([lo[i], lo[j], hi[j], hi[i]]))
    solid = cq.Solid.makeSolid(cq.Shell.makeShell(faces)).fix()
    return cq.Workplane("XY").add(solid)


def side_step(shift):
    """Sliver removed from the -X side face for y > STEP_Y (steeper face),
    moved inward by 'shift' for the inner skin."""
    top_x = -hw + DRAFT_IN + STEP_IN
    slope = (top_x + hw) / T
    wedge = (
        cq.Workplane("XZ")
        .polyline([
            (-hw - slope, -1.0),
            (top_x + slope, T + 1.0),
            (-hw - 6.0, T + 1.0),
            (-hw - 6.0, -1.0),
        ])
        .close()
        .extrude(-(hl + 5.0))        # XZ normal is -Y: negative extrudes toward +Y
    )
    half = (
        cq.Workplane("XY")
        .polyline([
            (-hw - 8.0, STEP_Y - 8.0),
            (-hw + 6.0, STEP_Y + 6.0),
            (-hw + 6.0, hl + 6.0),
            (-hw - 8.0, hl + 6.0),
        ])
        .close()
        .extrude(T + 4.0)
        .translate((0, 0, -2.0))
    )
    return wedge.intersect(half).translate((shift, 0, 0))


def channel(grow):
    """Channel tool: ruled loft between the top outline and the floor outline.
    'grow' offsets every channel surface outward (into the material)."""
    z_top = T + MARGIN
    depth = GROOVE_D + grow
    top_l, top_r, bot_l, bot_r = [], [], [], []
    for y, xl, xr, sl, sr in STATIONS:
        hl_ = math.hypot(sl, GROOVE_D)
        hr_ = math.hypot(sr, GROOVE_D)
        xl2 = xl - grow * hl_ / GROOVE_D      # bank planes shifted by grow
        xr2 = xr + grow * hr_ / GROOVE_D
        kl, kr = sl / GROOVE_D, sr / GROOVE_D  # horizontal run per unit depth
        top_l.append(cq.Vector(xl2 - kl * MARGIN, y, z_top))
        top_r.append(cq.Vector(xr2 + kr * MARGIN, y, z_top))
        bot_l.append(cq.Vector(xl2 + kl * depth, y, T - depth))
        bot_r.append(cq.Vector(xr2 - kr * depth, y, T - depth))

    def outline_wire(lpts, rpts):
        rr = list(reversed(rpts))
        return cq.Wire.assembleEdges([
            cq.Edge.makeSpline(lpts),
            cq.Edge.makeLine(lpts[-1], rr[0]),
            cq.Edge.makeSpline(rr),
            cq.Edge.makeLine(rr[-1], lpts[0]),
        ])

    solid = cq.Solid.makeLoft([outline_wire(top_l, top_r), outline_wire(bot_l, bot_r)], True)
    return cq.Workplane("XY").add(solid)


def round_both(body, z_top, r_left, r_right):
    """Round the two channel shoulder edges lying on the planar top at z_top:
    the -X one first, then the +X one (reselected after the first fillet)."""
    tops = [
        f for f in body.val().Faces()
        if f.geomType() == "PLANE" and abs(f.Center().z - z_top) < 1e-3
    ]
    edges = sorted(
        [e for f in tops for e in f.Edges() if e.geomType() == "BSPLINE"],
        key=lambda e: e.Center().x,
    )
    left, right = edges[0], edges[-1]
    if r_left > 0:
        body = body.newObject([left]).fillet(r_left)
    if r_right > 0:
        tops = [
            f for f in body.val().Faces()
            if f.geomType() == "PLANE" and abs(f.Center().z - z_top) < 1e-3
        ]
        cand = [e for f in tops for e in f.Edges() if e.geomType() == "BSPLINE"]
        right = max(cand, key=lambda e: e.Center().x)
        body = body.newObject([right]).fillet(r_right)
    return body


# ---------------- outer body ----------------
outer = slab(0.0, 0.0, T).cut(side_step(0.0)).cut(channel(0.0))
outer = round_both(outer, T, SHOULDER_R_LEFT, SHOULDER_R_RIGHT)

# ---------------- hollow underside (uniform skin) ----------------
if WALL > 0:
    step_cos = math.cos(math.atan2(DRAFT_IN + STEP_IN, T))
    cavity = (
        slab(WALL / cos_t, -1.0, T - WALL)
        .cut(side_step(WALL / step_cos))
        .cut(channel(WALL))
    )
    cavity = round_both(
        cavity, T - WALL,
        max(SHOULDER_R_LEFT - WALL, 0.0), max(SHOULDER_R_RIGHT - WALL, 0.0),
    )
    result = outer.cut(cavity)
else:
    result = outer
